import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 20.0          # thread crest radius (OD 40)
R_ROOT = 13.3         # thread root radius = hub radius
PITCH = 12.0          # lead of the single start, LEFT-hand thread
FLANK = 30.0          # flank half angle (deg)  -> 60 deg thread form
CREST = 1.6           # crest land width
L_HUB = 13.3          # plain hub length at the front (-Y)
L_THR = 33.0          # threaded length
L_CONE = 6.9          # rear chamfer cone length
R_CONE_END = 9.4      # rear end face radius
GROOVE_START = -3.0   # axial position of groove centre at its start (rel. to thread start)
GROOVE_TURNS = 3.6    # turns of the helical groove (runs out past the rear end)

BORE_D = 14.0         # front blind bore
BORE_DEPTH = 30.0
POINT_ANGLE = 90.0    # included angle of the bore bottom cone
CENTER_D = 2.6        # small centre recess at the bore bottom
CENTER_DEPTH = 1.5
PIN_D = 2.7           # small offset through hole (bore bottom -> rear face)
PIN_X = 2.4           # offset (world X)
PIN_Z = 2.3           # offset (world Z)

SEAM_ANGLE = 130.0    # where the periodic seams of revolved faces are parked (local deg)

# ---------------- derived ----------------
DEPTH = R_OUT - R_ROOT
T = math.tan(math.radians(FLANK))
ROOT_W = PITCH - CREST - 2 * DEPTH * T     # groove bottom width
Z0 = L_HUB                                  # thread start (local axis = Z)
Z1 = L_HUB + L_THR                          # thread end
ZE = Z1 + L_CONE                            # rear face

# Everything is built along local +Z, then rotated so that the axis is world +Y.
# (local X stays world X, local +Y becomes world -Z, i.e. the bottom)
ORG = cq.Vector(0, 0, 0)
ZAX = cq.Vector(0, 0, 1)


def cyl(r, h, z):
    return cq.Solid.makeCylinder(r, h, cq.Vector(0, 0, z), ZAX).rotate(ORG, ZAX, SEAM_ANGLE)


# core (hub + thread root cylinder) and rear cone
core = cyl(R_ROOT, Z1, 0.0)
cone = cq.Solid.makeCone(R_ROOT, R_CONE_END, L_CONE, cq.Vector(0, 0, Z1), ZAX).rotate(
    ORG, ZAX, SEAM_ANGLE
)

# thread blank ring, made longer than needed so that the groove ends inside it
EXTRA = 20.0
ring = cyl(R_OUT, L_THR + EXTRA, Z0).cut(cyl(R_ROOT, L_THR + EXTRA, Z0))

# helical groove: trapezoid in the meridian plane (local YZ) swept along a LH helix.
# It starts at the bottom (local +Y = world -Z) partly in front of the thread start,
# which produces the characteristic step where the thread begins.
zg = Z0 + GROOVE_START
r_in, r_ex = R_ROOT - 1.0, R_OUT + 1.5
hw_in = ROOT_W / 2 - (R_ROOT - r_in) * T
hw_ex = ROOT_W / 2 + (r_ex - R_ROOT) * T
prof = cq.Wire.makePolygon(
    [
        cq.Vector(0, r_in, zg - hw_in),
        cq.Vector(0, r_ex, zg - hw_ex),
        cq.Vector(0, r_ex, zg + hw_ex),
        cq.Vector(0, r_in, zg + hw_in),
    ],
    close=True,
)
helix = cq.Wire.makeHelix(
    PITCH, PITCH * GROOVE_TURNS, R_ROOT, cq.Vector(0, 0, zg), ZAX, lefthand=True
).rotate(ORG, ZAX, 90)
groove = cq.Solid.sweep(prof, [], helix, makeSolid=True, isFrenet=True)

thread = ring.cut(groove)
ring_vol = ring.Volume()
if not (0.3 * ring_vol < thread.Volume() < 0.9 * ring_vol):
    # fallback: cut the groove one turn at a time (screw symmetry -> pure translation)
    helix1 = cq.Wire.makeHelix(
        PITCH, PITCH, R_ROOT, cq.Vector(0, 0, zg), ZAX, lefthand=True
    ).rotate(ORG, ZAX, 90)
    turn = cq.Solid.sweep(prof, [], helix1, makeSolid=True, isFrenet=True)
    thread = ring
    for k in range(int(math.ceil(GROOVE_TURNS))):
        thread = thread.cut(turn.translate(cq.Vector(0, 0, k * PITCH)))
# trim the threaded ring to its real length
thread = thread.cut(cyl(R_OUT + 5.0, EXTRA + 5.0, Z1))

body = core.fuse(cone).fuse(thread).clean()

# front bore with conical bottom and a small flat centre recess
half = math.radians(POINT_ANGLE / 2)
z_c = BORE_DEPTH + (BORE_D / 2 - CENTER_D / 2) / math.tan(half)
bore_pts = [
    (0, -0.5),
    (BORE_D / 2, -0.5),
    (BORE_D / 2, BORE_DEPTH),
    (CENTER_D / 2, z_c),
    (CENTER_D / 2, z_c + CENTER_DEPTH),
    (0, z_c + CENTER_DEPTH),
]
# Workplane "XZ": sketch y is local Z; revolve about local Z
bore = (
    cq.Workplane("XZ")
    .polyline(bore_pts)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .val()
    .rotate(ORG, ZAX, SEAM_ANGLE)
)

# small offset through hole (world +X, +Z  ->  local +X, -Y)
pin = cq.Solid.makeCylinder(PIN_D / 2, ZE + 1.0, cq.Vector(PIN_X, -PIN_Z, -0.5), ZAX)

body = body.cut(bore).cut(pin)

# rotate so local +Z -> world +Y (local +Y -> world -Z)
body = body.rotate(ORG, cq.Vector(1, 0, 0), -90)

result = cq.Workplane("XY").add(body)
